import math
import cadquery as cq

# ------------------------------------------------------------------
# Twin-wing paddle craft: two hydrofoil wings, four octagonal paddles,
# a central equipment box with a pod below, and a tubular frame.
# All dimensions in mm.  +X = right, +Y = back, +Z = up.
# ------------------------------------------------------------------

Y_ST = 31.25          # Y position of the two drive lines (+/-)

# frame rods (main horizontal rods along X at Z = 0)
ROD_D = 1.8
ROD_X0, ROD_X1 = -69.0, 40.0
FIT_D, FIT_L = 3.8, 6.5        # cross fitting at the right rod end
ELB_D = 4.4                    # elbow fitting

# right (upper, +X) wing
RW_TE, RW_LE = 37.5, 67.5
RW_Z = 28.1
RW_TH = 0.12          # thickness / chord
RW_SPAN = 175.0

# left (lower, -X) wing
LW_TE, LW_LE = -64.25, -28.75
LW_Z = -21.8
LW_TH = 0.11
LW_SPAN = 237.5

# octagonal paddles
OCT_R = 29.3          # circumradius
OCT_T = 1.8           # plate thickness
HUB_D, HUB_L = 9.5, 5.5        # paddle hub
SLEEVE_D, SLEEVE_L = 4.2, 7.4  # axle sleeve next to the hub
POST_D, POST_OFF = 2.2, 2.5    # wing posts / struts on the sleeves
AXLE_D = 1.7                   # paddle axle diameter
L_AXLE_X0 = -68.3              # outer end of the left axles
ROCT_X, ROCT_Z = 68.9, 21.6
LOCT_X, LOCT_Z = -29.4, -29.5

# fins (small vertical stabilisers)
FIN_X0, FIN_X1 = -52.5, -32.5
FIN_Z0, FIN_Z1 = -17.5, 9.8
FIN_Y = 38.0
FIN_TH = 0.12
FIN_PIVOT_X = -37.7

# central box and pod
CX = 9.0
BOX_W, BOX_D, BOX_Z0, BOX_Z1 = 48.0, 48.0, 8.0, 32.0
BOX_R = 4.0          # corner radius of the XZ profile
BOX_DOME = 0.6       # rise of the domed lid
BOX_CH = 1.3         # chamfer round the front/back faces
POD_W, POD_D, POD_Z0, POD_Z1 = 45.0, 58.0, -21.8, -2.3
POD_CH_X, POD_CH_Y, POD_CH_Z = 7.0, 3.5, 4.3


# ------------------------------------------------------------------
# helpers
# ------------------------------------------------------------------
def cyl_x(x0, x1, y, z, d):
    pl = cq.Plane(origin=(x0, y, z), xDir=(0, 0, 1), normal=(1, 0, 0))
    return cq.Workplane(pl).circle(d / 2.0).extrude(x1 - x0)


def cyl_y(y0, y1, x, z, d):
    return (cq.Workplane("XZ").workplane(offset=-y1).center(x, z)
            .circle(d / 2.0).extrude(y1 - y0))


def hub_x(x0, x1, y, z, d, r):
    """axle hub: short cylinder along X with rounded rims"""
    return cyl_x(x0, x1, y, z, d).faces("<X or >X").edges().fillet(r)


def cyl_z(z0, z1, x, y, d):
    return (cq.Workplane("XY").workplane(offset=z0).center(x, y)
            .circle(d / 2.0).extrude(z1 - z0))


def naca_h(t, x):
    """symmetric NACA 00xx half thickness (fraction of chord)"""
    return 5 * t * (0.2969 * math.sqrt(x) - 0.1260 * x - 0.3516 * x ** 2
                    + 0.2843 * x ** 3 - 0.1036 * x ** 4)


def naca_dh(t, x):
    return 5 * t * (0.2969 / (2 * math.sqrt(x)) - 0.1260 - 0.7032 * x
                    + 0.8529 * x ** 2 - 0.4144 * x ** 3)


def airfoil_face(le_u, te_u, v0, t, x_nose=0.11):
    """airfoil face in the XY plane: chord along X (leading edge at le_u,
    rounded; trailing edge at te_u, sharp), thickness along Y about v0.
    Each surface is a main spline plus a tangent-continuous nose spline
    (x_nose = chord fraction of the split; None = single spline)."""
    sgn = 1.0 if le_u > te_u else -1.0
    c = abs(le_u - te_u)

    def P(x, side):
        return cq.Vector(le_u - sgn * x * c, v0 + side * naca_h(t, x) * c, 0)

    edges = []
    for side in (1.0, -1.0):
        t_te = cq.Vector(sgn, -side * naca_dh(t, 1.0), 0)
        t_le = cq.Vector(0, -side, 0)
        if x_nose is None:
            pts = ([cq.Vector(te_u, v0, 0)]
                   + [P(x, side) for x in (0.7, 0.45, 0.25, 0.1, 0.025)]
                   + [cq.Vector(le_u, v0, 0)])
            edges.append(cq.Edge.makeSpline(pts, tangents=[t_te, t_le]))
            continue
        # main surface from the trailing edge to x_nose, then the nose
        t_ln = cq.Vector(sgn, -side * naca_dh(t, x_nose), 0)
        body = ([cq.Vector(te_u, v0, 0)]
                + [P(x, side) for x in (0.75, 0.5, 0.3, x_nose)])
        nose = [P(x, side) for x in (x_nose, 0.05, 0.01)] + [cq.Vector(le_u, v0, 0)]
        edges.append(cq.Edge.makeSpline(body, tangents=[t_te, t_ln]))
        edges.append(cq.Edge.makeSpline(nose, tangents=[t_ln, t_le]))
    return cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))


def wing(te, le, z, t, span):
    f = airfoil_face(le, te, z, t)
    a = cq.Solid.extrudeLinear(f, cq.Vector(0, 0, span / 2.0))
    b = cq.Solid.extrudeLinear(f, cq.Vector(0, 0, -span / 2.0))
    sol = a.fuse(b).rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 90)
    return cq.Workplane("XY").add(sol)


def octagon(x, y, z):
    return (cq.Workplane("YZ").workplane(offset=x - OCT_T / 2.0)
            .center(y, z).polygon(8, 2 * OCT_R).extrude(OCT_T))


def fin(ysign):
    f = airfoil_face(FIN_X1, FIN_X0, ysign * FIN_Y, FIN_TH, None)
    sol = cq.Solid.extrudeLinear(f, cq.Vector(0, 0, FIN_Z1 - FIN_Z0))
    return cq.Workplane("XY").add(sol.translate(cq.Vector(0, 0, FIN_Z0)))


# ------------------------------------------------------------------
# wings
# ------------------------------------------------------------------
parts = []
parts.append(wing(RW_TE, RW_LE, RW_Z, RW_TH, RW_SPAN))
parts.append(wing(LW_TE, LW_LE, LW_Z, LW_TH, LW_SPAN))

# ------------------------------------------------------------------
# paddles, axles and frame for each drive line
# ------------------------------------------------------------------
def paddle_axle(xp, y, z, x_end):
    """octagonal paddle at plate-centre X = xp with its hub on the -X side,
    a sleeve next to the hub and an axle running from x_end to the plate.
    Returns the solids and the X of the strut/post position."""
    hub1 = xp - OCT_T / 2.0
    hub0 = hub1 - HUB_L
    sl0 = hub0 - SLEEVE_L
    out = [octagon(xp, y, z),
           cyl_x(xp - 1.0, xp + OCT_T / 2.0 + 0.4, y, z, 1.2),   # centre pin
           cyl_x(min(x_end, xp), max(x_end, xp), y, z, AXLE_D),  # axle
           cyl_x(sl0, hub0, y, z, SLEEVE_D),                     # sleeve
           hub_x(hub0, hub1, y, z, HUB_D, 1.2)]                  # hub
    return out, hub0 - POST_OFF


for s in (1.0, -1.0):
    y = s * Y_ST
    # --- right (upper) paddle, fed by a riser and elbow from the rod end
    sol, x_post = paddle_axle(ROCT_X, y, ROCT_Z, ROD_X1)
    parts += sol
    parts.append(cyl_z(ROCT_Z, RW_Z, x_post, y, POST_D))        # wing post
    # main rod with a cross fitting at its right end
    parts.append(cyl_x(ROD_X0, ROD_X1, y, 0.0, ROD_D))
    parts.append(cyl_x(ROD_X1 - FIT_L, ROD_X1 + FIT_L, y, 0.0, FIT_D))
    parts.append(cyl_z(-FIT_L, FIT_L, ROD_X1, y, FIT_D))
    # riser and elbow up to the right axle
    parts.append(cyl_z(0.0, ROCT_Z, ROD_X1, y, ROD_D))
    parts.append(cyl_z(ROCT_Z - 5.0, ROCT_Z, ROD_X1, y, ELB_D))
    parts.append(cyl_x(ROD_X1, ROD_X1 + 5.0, y, ROCT_Z, ELB_D))
    parts.append(cq.Workplane("XY").sphere(ELB_D / 2.0)
                 .translate((ROD_X1, y, ROCT_Z)))

    # --- left (lower) paddle on an axle running out to -X
    sol, x_strut = paddle_axle(LOCT_X, y, LOCT_Z, L_AXLE_X0)
    parts += sol
    # strut from the axle sleeve up through the wing to the main rod
    parts.append(cyl_z(LOCT_Z, 0.0, x_strut, y, POST_D))

    # --- fin with its pivot pin, rod sleeve and foot on the wing
    parts.append(fin(s))
    fo = s * (FIN_Y + 1.6)
    parts.append(cyl_y(min(y, fo), max(y, fo), FIN_PIVOT_X, 0.0, 1.2))
    parts.append(cyl_x(FIN_X0 + 8.5, LOCT_X - 1.0, y, 0.0, 3.4))
    parts.append(cq.Workplane("XY").box(2.5, 2.0, FIN_Z0 - LW_Z + 0.5)
                 .translate((FIN_PIVOT_X, s * FIN_Y, (FIN_Z0 + LW_Z) / 2.0)))

    # --- tee on the rod under the box and a pod hanger
    parts.append(cyl_x(CX - 6.5, CX + 6.5, y, 0.0, 3.7))
    parts.append(cyl_y(min(y, y - s * 5.0), max(y, y - s * 5.0), CX, 0.0, 3.7))
    parts.append(cyl_z(POD_Z1 - 1.0, 0.0, CX, s * 12.0, 2.4))

# cross bar between the tees and the central stem up to the box
parts.append(cyl_y(-Y_ST, Y_ST, CX, 0.0, ROD_D))
parts.append(cyl_z(0.0, BOX_Z0 + 1.5, CX, 0.0, 5.3))
parts.append(cyl_z(BOX_Z0 - 1.5, BOX_Z0 + 1.0, CX, 0.0, 8.0))

# ------------------------------------------------------------------
# equipment box
# ------------------------------------------------------------------
def box_body():
    """equipment box: XZ section with rounded shoulders and a slightly
    domed lid (smooth splines) and straight sides, extruded along Y"""
    a = BOX_W / 2.0
    b = (BOX_Z1 - BOX_Z0 - BOX_DOME) / 2.0
    zc = BOX_Z0 + b
    r = BOX_R

    def arc(cx, cz, a0, a1):
        return [(cx + r * math.cos(math.radians(a0 + (a1 - a0) * k / 3.0)),
                 cz + r * math.sin(math.radians(a0 + (a1 - a0) * k / 3.0)))
                for k in range(4)]

    top = (arc(a - r, b - r, 0, 90)
           + [(x, b + BOX_DOME * (1 - (x / (a - r)) ** 2))
              for x in (0.5 * (a - r), 0.0, -0.5 * (a - r))]
           + arc(-(a - r), b - r, 90, 180))
    bot = (arc(-(a - r), -(b - r), 180, 270)
           + [(x, -b) for x in (-0.5 * (a - r), 0.0, 0.5 * (a - r))]
           + arc(a - r, -(b - r), 270, 360))

    def V(p):
        return cq.Vector(CX + p[0], zc + p[1], 0)

    up, dn = cq.Vector(0, 1, 0), cq.Vector(0, -1, 0)
    edges = [cq.Edge.makeSpline([V(p) for p in top], tangents=[up, dn], scale=False),
             cq.Edge.makeLine(V(top[-1]), V(bot[0])),
             cq.Edge.makeSpline([V(p) for p in bot], tangents=[dn, up], scale=False),
             cq.Edge.makeLine(V(bot[-1]), V(top[0]))]
    face = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
    sol = (cq.Solid.extrudeLinear(face, cq.Vector(0, 0, BOX_D))
           .translate(cq.Vector(0, 0, -BOX_D / 2.0))
           .rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 90))
    # small chamfer all round the front and back faces
    return cq.Workplane("XY").add(sol).faces("<Y or >Y").edges().chamfer(BOX_CH)


box = box_body()
parts.append(box)

# ------------------------------------------------------------------
# pod: elliptic section (YZ) along X with chamfered (lofted) ends
# ------------------------------------------------------------------
pa, pb = POD_D / 2.0, (POD_Z1 - POD_Z0) / 2.0
pzc = (POD_Z0 + POD_Z1) / 2.0
pod = (cq.Workplane("YZ").workplane(offset=CX - POD_W / 2.0).center(0, pzc)
       .ellipse(pa - POD_CH_Y, pb - POD_CH_Z)
       .workplane(offset=POD_CH_X).ellipse(pa, pb)
       .workplane(offset=POD_W - 2 * POD_CH_X).ellipse(pa, pb)
       .workplane(offset=POD_CH_X).ellipse(pa - POD_CH_Y, pb - POD_CH_Z)
       .loft(ruled=True))
parts.append(pod)

# ------------------------------------------------------------------
result = parts[0]
for p in parts[1:]:
    result = result.union(p)

VIEW = {"azimuth": 45, "elevation": 26}
